import cadquery as cq

# Filament swatch card: full-round perimeter, recessed label field with
# embossed text, raised platform holding a 5-step thickness pocket.

# ---------------- driving dimensions (mm) ----------------
L = 80.0            # card length (X)
W = 34.6            # card width  (Y)
T = 2.0             # card thickness (Z)
R_CORNER = 3.3      # plan-view corner radius (full round edge radius = T/2)

RIM = 2.35          # flat ledge width between outer edge and recessed field
FIELD_DEPTH = 0.75  # depth of the recessed label field

# platform in the lower-right quadrant (stays at ledge height)
PLAT_X0 = 0.0       # left edge of the platform
PLAT_Y1 = -2.5      # top edge of the platform

# stepped thickness pocket inside the platform
POCKET_MARGIN = 2.5         # platform frame width left/top of the pocket
N_STEPS = 5
STEP_DEPTH0 = 1.2           # depth of the shallowest (left) cell
STEP_INC = 0.15             # extra depth per cell (deeper towards +X)

# embossed text
TEXT_H = 0.5        # emboss height above the field floor (stays below rim)
FONT = "DejaVu Sans"
TEXT_INSET = 1.65   # left margin of the left text column inside the field

FX = L / 2.0 - RIM  # field half-length
FY = W / 2.0 - RIM  # field half-width

# ---------------- base slab with full-round perimeter ----------------
# inner core (rounded rectangle inset by half the thickness) plus a half-disc
# profile swept around its outline -> full round edge
r_round = T / 2.0
Li, Wi, Ri = L - T, W - T, R_CORNER - r_round
path = cq.Wire.makePolygon(
    [
        cq.Vector(Li / 2, -Wi / 2, r_round),
        cq.Vector(Li / 2, Wi / 2, r_round),
        cq.Vector(-Li / 2, Wi / 2, r_round),
        cq.Vector(-Li / 2, -Wi / 2, r_round),
    ],
    close=True,
).fillet(Ri)
x0, y0 = Li / 2, -Wi / 2 + Ri          # start point of the path (straight edge)
half_disc = cq.Wire.assembleEdges(
    [
        cq.Edge.makeThreePointArc(
            cq.Vector(x0, y0, T), cq.Vector(x0 + r_round, y0, r_round), cq.Vector(x0, y0, 0)
        ),
        cq.Edge.makeLine(cq.Vector(x0, y0, 0), cq.Vector(x0, y0, T)),
    ]
)
rim_ring = cq.Workplane("XY").add(half_disc).toPending().sweep(cq.Workplane("XY").add(path))
core = cq.Workplane("XY").sketch().rect(Li, Wi).vertices().fillet(Ri).finalize().extrude(T)
base = core.union(rim_ring, clean=True)

# ---------------- recessed label field (L-shaped, platform excluded) ----------------
field_pts = [
    (-FX, -FY),
    (PLAT_X0, -FY),
    (PLAT_X0, PLAT_Y1),
    (FX, PLAT_Y1),
    (FX, FY),
    (-FX, FY),
]
field_cut = (
    cq.Workplane("XY")
    .workplane(offset=T - FIELD_DEPTH)
    .polyline(field_pts)
    .close()
    .extrude(FIELD_DEPTH + 1.0)
)
body = base.cut(field_cut)

# ---------------- stepped pocket (5 thickness samples) ----------------
px0 = PLAT_X0 + POCKET_MARGIN
px1 = FX
py0 = -FY
py1 = PLAT_Y1 - POCKET_MARGIN
cell_w = (px1 - px0) / N_STEPS
for i in range(N_STEPS):
    d = STEP_DEPTH0 + STEP_INC * i
    cx = px0 + cell_w * (i + 0.5)
    cell = (
        cq.Workplane("XY")
        .workplane(offset=T - d)
        .center(cx, (py0 + py1) / 2.0)
        .rect(cell_w, py1 - py0)
        .extrude(d + 1.0)
    )
    body = body.cut(cell)

# ---------------- embossed text on the field floor ----------------
z_floor = T - FIELD_DEPTH
x_left = -FX + TEXT_INSET
texts = [
    # (string, font size, horizontal stretch, x origin, baseline y)
    ("Green", 7.5, 1.0, x_left + 0.1, FY - 8.4),
    ("Creality", 5.3, 1.08, x_left, -7.2),
    ("PLA-HS", 5.17, 1.10, x_left, -FY + 1.85),
    ("N215°", 5.65, 1.083, -4.1, -0.95),
    ("B60°", 5.65, 1.083, 19.6, -0.95),
]
for s, size, sx, x, y in texts:
    glyphs = (
        cq.Workplane("XY")
        .text(s, size, TEXT_H, font=FONT, kind="bold",
              halign="left", valign="bottom", combine=False)
        .val()
    )
    if abs(sx - 1.0) > 1e-9:
        glyphs = glyphs.transformGeometry(
            cq.Matrix([[sx, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0], [0, 0, 0, 1]])
        )
    glyphs = glyphs.translate(cq.Vector(x, y, z_floor))
    body = body.union(cq.Workplane("XY").add(glyphs))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
